import cadquery as cq
import math

# ------------------------------------------------------------------
# Dump truck model standing on its tail.
#   X : lateral (width), centred on 0
#   Y : truck "up"  (roof / open top of dump bed at +Y, chassis at -Y)
#   Z : truck length (front bumper at +Z, tailgate at Z = 0)
# ------------------------------------------------------------------

# --- overall / chassis ---
RAIL_X0, RAIL_X1 = 15.8, 18.8          # rear frame rails (|X| range)
FRAIL_X0, FRAIL_X1 = 9.4, 12.8         # front frame rails (narrower, under the hood)
RAIL_JOG_Z = 160.0                     # frame joggle (under the cab)
RAIL_Y0, RAIL_Y1 = -12.4, -4.3
RAIL_Z0, RAIL_Z1 = 1.0, 234.5

# --- dump bed ---
BED_W = 39.0          # half width (outside of side walls)
BED_H = 42.0          # side wall height (Y)
BED_L = 131.8         # length (Z) up to the headboard
BED_T = 2.4           # wall / floor thickness
RIB_Z = [24.0, 44.5, 65.0, 85.5, 106.0]
HEAD_Z0, HEAD_Z1 = 129.3, 135.8        # headboard incl. edge posts
HEAD_TOP = 62.0
HEAD_ROLL_R = 2.5
TOP_RAIL_R = 2.0

# --- cab protector ---
PROT_W = 36.3
PROT_Y0, PROT_Y1 = 55.0, 57.1
PROT_Z0, PROT_Z1 = 135.8, 168.8
BRACE_Y0, BRACE_Z1 = 38.7, 146.6       # slanted brace: from headboard (Y) to protector (Z)

# --- cab ---
CAB_Z0, CAB_Z1 = 140.5, 181.0
CAB_W = 35.5
STEP_W = 42.7
CAB_Y0 = -23.0
BELT_Y = 22.0
ROOF_Y = 48.5
ROOF_FILLET = 5.0
BODY_W = 30.5                          # door / greenhouse half width at the belt line
GREEN_W1 = 28.5                        # greenhouse half width at the roof
SILL_Y = -3.0                          # top of the wide cab floor section
WS_W = 27.0                            # windshield half width

# --- hood ---
HOOD_Z0, HOOD_Z1 = 181.0, 233.8
HOOD_Y0, HOOD_TOP = -10.9, 25.6
FENDER_W = 37.2
HOOD_W = 29.7
HOOD_NOSE_W = 18.5
HOOD_TAPER_Z = 195.0      # hood sides start to curve in towards the nose here
HR = 7.0                  # hood shoulder radius
NOSE_Y0, NOSE_Y1 = 10.5, 22.3   # nose rounding: from front face to hood top
NOSE_Z1 = 210.0
FENDER_IN = 22.0
FENDER_Z1 = 228.0
FENDER_ARCH_R = 26.0
FENDER_FILLET = 4.5
WELL_R = 20.0
GRILLE_W = 14.1

# --- wheels ---
WHEEL_R = 16.4
WHEEL_Y = -18.2
FRONT_AXLE_Z = 205.5
REAR_AXLE_Z = [65.5, 30.9]
TIRE_X0, TIRE_X1 = 20.0, 37.4          # front tyre |X| range
DUAL_X = [(19.8, 28.6), (29.4, 38.2)]  # rear dual tyres |X| ranges
TIRE_FILLET = 4.0

# --- bumper ---
BUMP_Y0, BUMP_Y1 = -20.4, -8.8
BUMP_ZF = 237.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_x(x0, x1, yc, zc, r):
    return (cq.Workplane("YZ").workplane(offset=x0)
            .center(yc, zc).circle(r).extrude(x1 - x0))


def cyl_z(z0, z1, xc, yc, r):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(xc, yc).circle(r).extrude(z1 - z0))


def mirror_x(shape):
    return shape.union(shape.mirror("YZ"))


# ------------------------------------------------------------------
# wheels
# ------------------------------------------------------------------
def tire(x0, x1, yc, zc, r, outer_positive):
    """Tyre with rounded shoulders; dished rim with hub on the outer face and
    a plain dished rim (brake drum side) on the inner face."""
    w = x1 - x0
    t = cyl_x(x0, x1, yc, zc, r).edges("%CIRCLE").fillet(min(TIRE_FILLET, w * 0.36))
    depth = 2.0
    rr = r * 0.66
    xo, xi = (x1, x0) if outer_positive else (x0, x1)
    so = 1.0 if outer_positive else -1.0       # direction pointing out of the outer face

    def slab(a, b, rad):
        lo, hi = min(a, b), max(a, b)
        return cyl_x(lo, hi, yc, zc, rad)

    # outer face: rim dish, hub and cap
    t = t.cut(slab(xo - so * depth, xo + so * 1.0, rr))
    t = t.union(slab(xo - so * (depth + 0.5), xo - so * 0.6, r * 0.42))
    t = t.union(slab(xo - so * 1.0, xo - so * 0.2, r * 0.2))
    # inner face: shallower dish with brake drum
    t = t.cut(slab(xi + so * 1.4, xi - so * 1.0, rr * 0.95))
    t = t.union(slab(xi + so * 1.6, xi + so * 0.5, r * 0.36))
    return t


parts = []

# front wheels + axle
for s in (1, -1):
    if s > 0:
        parts.append(tire(TIRE_X0, TIRE_X1, WHEEL_Y, FRONT_AXLE_Z, WHEEL_R, True))
    else:
        parts.append(tire(-TIRE_X1, -TIRE_X0, WHEEL_Y, FRONT_AXLE_Z, WHEEL_R, False))
parts.append(cyl_x(-TIRE_X0 - 0.5, TIRE_X0 + 0.5, WHEEL_Y, FRONT_AXLE_Z, 1.8))
parts.append(cyl_x(-TIRE_X0 + 1, TIRE_X0 - 1, WHEEL_Y + 2.5, FRONT_AXLE_Z + 5.0, 0.8))
for s in (1, -1):
    parts.append(box(s * FRAIL_X0 if s > 0 else -FRAIL_X1, s * FRAIL_X1 if s > 0 else -FRAIL_X0,
                     WHEEL_Y, -15.0, FRONT_AXLE_Z - 2.0, FRONT_AXLE_Z + 2.0))

# rear tandem axles with dual wheels and differentials
for za in REAR_AXLE_Z:
    for (a, b) in DUAL_X:
        parts.append(tire(a, b, WHEEL_Y, za, WHEEL_R, b > 30))
        parts.append(tire(-b, -a, WHEEL_Y, za, WHEEL_R, not (b > 30)))
    parts.append(cyl_x(-DUAL_X[0][0] - 0.5, DUAL_X[0][0] + 0.5, WHEEL_Y, za, 2.3))
    for s in (1, -1):
        parts.append(cyl_x(s * 27.5 if s > 0 else -30.5, s * 30.5 if s > 0 else -27.5,
                           WHEEL_Y, za, WHEEL_R * 0.42))
    # differential "pumpkin": bulb plus a conical pinion housing pointing forward
    parts.append(cq.Workplane("XY").sphere(4.6).translate((0, WHEEL_Y, za)))
    parts.append(cq.Workplane("XY").add(cq.Solid.makeCone(
        4.0, 1.7, 8.5, cq.Vector(0, WHEEL_Y + 0.6, za + 0.5), cq.Vector(0, 0, 1))))
    # spring hangers / leaf springs under the rails
    for s in (1, -1):
        parts.append(box(s * RAIL_X0 if s > 0 else -RAIL_X1,
                         s * RAIL_X1 if s > 0 else -RAIL_X0,
                         WHEEL_Y + 1.5, RAIL_Y0, za - 12, za + 12))

# drive shafts
SHAFT_Y = -6.5
parts.append(cyl_z(REAR_AXLE_Z[0] + 20.0, CAB_Z0 + 2, 0, SHAFT_Y, 1.2))


def rod(p0, p1, r):
    v = cq.Vector(p1[0] - p0[0], p1[1] - p0[1], p1[2] - p0[2])
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(r, v.Length, cq.Vector(*p0), v.normalized()))


parts.append(rod((0, SHAFT_Y, REAR_AXLE_Z[0] + 20.5), (0, WHEEL_Y + 1.0, REAR_AXLE_Z[0] + 7.0), 1.2))
parts.append(cyl_z(REAR_AXLE_Z[1] + 7.0, REAR_AXLE_Z[0] - 2.5, 0, WHEEL_Y + 1.7, 1.1))

# ------------------------------------------------------------------
# frame
# ------------------------------------------------------------------
frame = box(RAIL_X0, RAIL_X1, RAIL_Y0, RAIL_Y1, RAIL_Z0, RAIL_JOG_Z + 2.0)          # rear rail
frame = frame.union(box(FRAIL_X0, FRAIL_X1, RAIL_Y0, RAIL_Y1, RAIL_JOG_Z - 2.0, RAIL_Z1))  # front rail
frame = frame.union(box(FRAIL_X0, RAIL_X1, RAIL_Y0, RAIL_Y1, RAIL_JOG_Z - 2.0, RAIL_JOG_Z + 2.0))
frame = mirror_x(frame)
for zc in (8.0, 24.0, 50.0, 127.0):
    frame = frame.union(box(-RAIL_X0, RAIL_X0, RAIL_Y0 + 2, RAIL_Y1, zc - 1.5, zc + 1.5))
frame = frame.union(box(-FRAIL_X0, FRAIL_X0, RAIL_Y0 + 2, RAIL_Y1, 224.5, 227.5))
parts.append(frame)
# bed sills
sill = mirror_x(box(RAIL_X0, RAIL_X1, RAIL_Y1, 0.0, 0.0, HEAD_Z0))
parts.append(sill)
# engine sump
parts.append(box(-8.0, 8.0, -14.0, HOOD_Y0 + 0.5, 196.6, 212.0))

# rear cross member with mud-flap brackets, and the under-ride guard
parts.append(box(-38.0, 38.0, -11.0, -8.0, 0.6, 4.6))
for s in (1, -1):
    parts.append(box(s * 37.5 - 2.0, s * 37.5 + 2.0, -11.0, -1.3, 0.6, 6.5))
UR_W = 27.0
parts.append(box(-UR_W, UR_W, -25.0, -23.4, 1.0, 3.6))
for s in (1, -1):
    parts.append(box(s * 13.0 - 1.0, s * 13.0 + 1.0, -23.6, -10.8, 1.5, 3.1))

# fuel tank (cylinder along Z, left side)
TANK_X, TANK_Y, TANK_R = -33.5, -9.7, 6.0
TANK_Z0, TANK_Z1 = 109.7, 136.6
tank = cyl_z(TANK_Z0, TANK_Z1, TANK_X, TANK_Y, TANK_R).faces("<Z or >Z").edges().fillet(1.2)
for zb in (TANK_Z0 + 2.8, TANK_Z0 + 5.3, TANK_Z1 - 5.3, TANK_Z1 - 2.8):
    tank = tank.union(cyl_z(zb - 0.5, zb + 0.5, TANK_X, TANK_Y, TANK_R + 0.4))
parts.append(tank)
parts.append(box(-RAIL_X1 - 9.0, -RAIL_X1, -8.0, -5.0, TANK_Z0 + 4.0, TANK_Z0 + 7.0))
parts.append(box(-RAIL_X1 - 9.0, -RAIL_X1, -8.0, -5.0, TANK_Z1 - 7.0, TANK_Z1 - 4.0))

# ------------------------------------------------------------------
# dump bed
# ------------------------------------------------------------------
bed = box(-BED_W, BED_W, 0.0, BED_T, 0.0, HEAD_Z0)                    # floor
for s in (1, -1):
    x0, x1 = (BED_W - BED_T, BED_W) if s > 0 else (-BED_W, -BED_W + BED_T)
    bed = bed.union(box(x0, x1, 0.0, BED_H - TOP_RAIL_R, 0.0, HEAD_Z0))   # side
    # rolled top rail (round bar along the side top edge)
    bed = bed.union(cyl_z(-0.6, HEAD_Z0 + 0.5, s * (BED_W - BED_T / 2.0), BED_H - TOP_RAIL_R, TOP_RAIL_R))
    ox0, ox1 = (BED_W, BED_W + 1.0) if s > 0 else (-BED_W - 1.0, -BED_W)
    bed = bed.union(box(ox0, ox1, 0.0, BED_T + 0.4, 0.0, HEAD_Z0))      # bottom rail
    for zr in RIB_Z:
        bed = bed.union(box(ox0, ox1, BED_T, BED_H - 2 * TOP_RAIL_R, zr - 1.0, zr + 1.0))
    # rear corner posts
    px0, px1 = (BED_W - 2.5, BED_W + 1.2) if s > 0 else (-BED_W - 1.2, -BED_W + 2.5)
    bed = bed.union(box(px0, px1, 0.0, BED_H - TOP_RAIL_R, 0.0, 4.0))
# tailgate
bed = bed.union(box(-BED_W + BED_T, BED_W - BED_T, BED_T, BED_H - TOP_RAIL_R, 1.0, 3.5))
for xr in (-13.4, 13.4):
    bed = bed.union(box(xr - 1.0, xr + 1.0, BED_T, BED_H - 1.0, 0.0, 1.0))
bed = bed.union(box(-BED_W, BED_W, 0.0, BED_T + 0.5, 0.0, 1.0))
# headboard
bed = bed.union(box(-BED_W, BED_W, 0.0, HEAD_TOP, HEAD_Z0, HEAD_Z0 + 2.5))
for s in (1, -1):
    px0, px1 = (BED_W - 2.2, BED_W) if s > 0 else (-BED_W, -BED_W + 2.2)
    bed = bed.union(box(px0, px1, 0.0, HEAD_TOP, HEAD_Z0, HEAD_Z1))
bed = bed.union(cyl_x(-BED_W - 0.8, BED_W + 0.8, HEAD_TOP + 2.0, HEAD_Z0 + 3.6, HEAD_ROLL_R))
parts.append(bed)

# cab protector: roof plate over the cab, braced by a full-width slanted panel
# running down to the headboard (closed triangular section)
prot = box(-PROT_W, PROT_W, PROT_Y0, PROT_Y1, HEAD_Z0 + 2.5, PROT_Z1)
brace = (cq.Workplane("YZ").workplane(offset=-PROT_W)
         .polyline([(BRACE_Y0, HEAD_Z0 + 2.5), (PROT_Y0 + 0.5, BRACE_Z1),
                    (PROT_Y0 + 0.5, BRACE_Z1 + 2.0), (BRACE_Y0 - 1.4, HEAD_Z0 + 2.5)])
         .close().extrude(2 * PROT_W))
prot = prot.union(brace)
parts.append(prot)

# ------------------------------------------------------------------
# cab
# ------------------------------------------------------------------
# wide floor / sill section
cab = box(-CAB_W, CAB_W, CAB_Y0, SILL_Y, CAB_Z0, CAB_Z1).edges("|Z").fillet(2.0)
# body (doors) + greenhouse, narrower than the sill
upper = (cq.Workplane("XY").workplane(offset=CAB_Z0)
         .polyline([(-BODY_W, SILL_Y - 0.5), (BODY_W, SILL_Y - 0.5), (BODY_W, BELT_Y),
                    (GREEN_W1, ROOF_Y), (-GREEN_W1, ROOF_Y), (-BODY_W, BELT_Y)])
         .close().extrude(CAB_Z1 + 1 - CAB_Z0))
ws = (cq.Workplane("YZ").workplane(offset=-40)
      .polyline([(SILL_Y - 2, CAB_Z0 - 1), (SILL_Y - 2, CAB_Z1), (20.8, CAB_Z1),
                 (45.7, 175.5), (ROOF_Y + 1, 173.0), (ROOF_Y + 1, CAB_Z0 - 1)])
      .close().extrude(80))
upper = upper.intersect(ws)
upper = upper.edges(">Y").edges("|Z").fillet(ROOF_FILLET)
cab = cab.union(upper)
# side windows (shallow recesses)
for s in (1, -1):
    xw = s * (BODY_W + GREEN_W1) / 2.0
    cab = cab.cut(box(xw - 2.0, xw + 2.0, 25.0, 43.0, 151.3, 172.0))
# windshield recess
cab = cab.cut(
    cq.Workplane("YZ").workplane(offset=-WS_W)
    .polyline([(24.5, 182.0), (43.5, 177.4), (43.5, 175.0), (24.5, 179.6)])
    .close().extrude(2 * WS_W))
# door seams + handles
for s in (1, -1):
    xs = s * BODY_W
    cab = cab.cut(box(xs - 0.6, xs + 0.6, SILL_Y, BELT_Y, 145.0, 145.8))
    cab = cab.cut(box(xs - 0.6, xs + 0.6, SILL_Y, BELT_Y, 176.2, 177.0))
    cab = cab.union(box(xs - 0.6, xs + 0.6, 3.0, 10.0, 153.4, 154.8))
parts.append(cab)

# side steps / battery boxes (rounded outer edges, groove next to the cab)
for s in (1, -1):
    x0, x1 = (CAB_W - 0.5, STEP_W) if s > 0 else (-STEP_W, -CAB_W + 0.5)
    stepb = box(x0, x1, CAB_Y0, -3.0, 143.0, 179.0)
    stepb = stepb.edges("|Z").edges(">X" if s > 0 else "<X").fillet(4.0)
    g0, g1 = (36.6, 38.0) if s > 0 else (-38.0, -36.6)
    stepb = stepb.cut(box(g0, g1, CAB_Y0 - 1, CAB_Y0 + 0.8, 146.0, 176.0))
    parts.append(stepb)

# exhaust stack behind the cab (left side): pipe, muffler and bent tip
EX_X, EX_Z = -39.0, 138.2
EX_TOP = 44.0
parts.append(cq.Workplane("XZ").workplane(offset=-SILL_Y)
             .center(EX_X, EX_Z).circle(1.0).extrude(-(EX_TOP - SILL_Y)))
parts.append(cq.Workplane("XZ").workplane(offset=-6.0)
             .center(EX_X, EX_Z).circle(2.2).extrude(-32.0))
for yb in (4.0, 34.0):
    parts.append(box(EX_X - 1.0, -BODY_W + 0.5, yb, yb + 2.0, EX_Z - 1.0, EX_Z + 1.0))
    parts.append(box(EX_X - 1.0, EX_X + 1.0, yb, yb + 2.0, HEAD_Z1 - 0.5, CAB_Z0 + 0.5))
tip = (cq.Workplane("XZ", origin=(0, EX_TOP, 0)).moveTo(EX_X, EX_Z).circle(1.0)
       .revolve(60, (EX_X - 3.0, 0, 0), (EX_X - 3.0, 1, 0)))
parts.append(tip)

# mirrors: tall head with an L-shaped arm to the door
for s in (1, -1):
    m0, m1 = (33.4, 38.3) if s > 0 else (-38.3, -33.4)
    parts.append(box(m0, m1, 21.3, 40.5, 171.5, 174.0).edges("|Z").fillet(1.0))
    a0, a1 = (35.0, 36.4) if s > 0 else (-36.4, -35.0)
    parts.append(box(a0, a1, 16.5, 21.8, 172.0, 173.4))
    b0, b1 = (BODY_W - 0.5, 36.4) if s > 0 else (-36.4, -BODY_W + 0.5)
    parts.append(box(b0, b1, 16.5, 17.9, 172.0, 173.4))

# front fender rear flaps
for s in (1, -1):
    f0, f1 = (TIRE_X0, FENDER_W) if s > 0 else (-FENDER_W, -TIRE_X0)
    parts.append(box(f0, f1, CAB_Y0 - 1.0, -1.5, CAB_Z1, CAB_Z1 + 3.5))

# ------------------------------------------------------------------
# hood with integrated fenders
# ------------------------------------------------------------------
def arc_mid(cx, cy, r, ang_deg):
    a = math.radians(ang_deg)
    return (cx + r * math.cos(a), cy + r * math.sin(a))


# hood centre body: cross-section (XY) with large rounded shoulders
hc_xy = (cq.Workplane("XY").workplane(offset=HOOD_Z0)
         .moveTo(-HOOD_W, HOOD_Y0)
         .lineTo(HOOD_W, HOOD_Y0)
         .lineTo(HOOD_W, HOOD_TOP - HR)
         .threePointArc(arc_mid(HOOD_W - HR, HOOD_TOP - HR, HR, 45), (HOOD_W - HR, HOOD_TOP))
         .lineTo(-HOOD_W + HR, HOOD_TOP)
         .threePointArc(arc_mid(-HOOD_W + HR, HOOD_TOP - HR, HR, 135), (-HOOD_W, HOOD_TOP - HR))
         .close()
         .extrude(HOOD_Z1 - HOOD_Z0))
# side profile (YZ): rounded nose, top rising towards the cab
hc_yz = (cq.Workplane("YZ").workplane(offset=-50)
         .moveTo(HOOD_Y0 - 1, HOOD_Z0 - 1)
         .lineTo(HOOD_Y0 - 1, HOOD_Z1)
         .lineTo(NOSE_Y0, HOOD_Z1 - 1.2)
         .spline([(NOSE_Y0 + 7.0, HOOD_Z1 - 4.6), (NOSE_Y0 + 10.6, HOOD_Z1 - 12.4),
                  (NOSE_Y1, NOSE_Z1)],
                 tangents=[(1.0, 0.0), (0.09, -1.0)], includeCurrent=True)
         .lineTo(HOOD_TOP - 0.6, HOOD_Z0 - 1)
         .close()
         .extrude(100))
# plan profile (XZ): sides curve in towards the narrow nose
PLAN_R = ((HOOD_W - HOOD_NOSE_W) ** 2 + (HOOD_Z1 - HOOD_TAPER_Z) ** 2) / (2.0 * (HOOD_W - HOOD_NOSE_W))
_cx = HOOD_W - PLAN_R
_ang = math.atan2(HOOD_Z1 - HOOD_TAPER_Z, HOOD_NOSE_W - _cx) / 2.0
_mid = (_cx + PLAN_R * math.cos(_ang), HOOD_TAPER_Z + PLAN_R * math.sin(_ang))
hc_xz = (cq.Workplane("XZ").workplane(offset=-(HOOD_TOP + 3))
         .moveTo(-HOOD_W, HOOD_Z0 - 1)
         .lineTo(HOOD_W, HOOD_Z0 - 1)
         .lineTo(HOOD_W, HOOD_TAPER_Z)
         .threePointArc(_mid, (HOOD_NOSE_W, HOOD_Z1))
         .lineTo(-HOOD_NOSE_W, HOOD_Z1)
         .threePointArc((-_mid[0], _mid[1]), (-HOOD_W, HOOD_TAPER_Z))
         .close()
         .extrude(HOOD_TOP - HOOD_Y0 + 6))
hood = hc_xy.intersect(hc_yz).intersect(hc_xz)

# fenders: arched over the front wheels, rounded outer edge
for s in (1, -1):
    fd = box(FENDER_IN, FENDER_W, HOOD_Y0, 40.0, HOOD_Z0, FENDER_Z1).intersect(
        cyl_x(FENDER_IN - 1, FENDER_W + 1, WHEEL_Y, FRONT_AXLE_Z, FENDER_ARCH_R))
    fd = fd.faces(">X").edges("not %LINE").fillet(FENDER_FILLET)
    if s < 0:
        fd = fd.mirror("YZ")
    hood = hood.union(fd)

# wheel wells
for s in (1, -1):
    a0, a1 = (TIRE_X0 - 1.0, FENDER_W + 2) if s > 0 else (-FENDER_W - 2, -TIRE_X0 + 1.0)
    hood = hood.cut(cyl_x(a0, a1, WHEEL_Y, FRONT_AXLE_Z, WELL_R))
# wheel-arch flare lips
for s in (1, -1):
    x0, x1 = (FENDER_W - 1.0, FENDER_W + 0.6) if s > 0 else (-FENDER_W - 0.6, -FENDER_W + 1.0)
    lip = cyl_x(x0, x1, WHEEL_Y, FRONT_AXLE_Z, WELL_R + 3.0).cut(
        cyl_x(x0 - 1, x1 + 1, WHEEL_Y, FRONT_AXLE_Z, WELL_R))
    lip = lip.intersect(box(-60, 60, HOOD_Y0, 40, HOOD_Z0, FENDER_Z1))
    hood = hood.union(lip)
# side vents on the hood flanks
for s in (1, -1):
    for k in range(4):
        zc = 193.5 + k * 3.2
        hood = hood.cut(box(s * HOOD_W - 0.7, s * HOOD_W + 0.7, 12.3, 16.0, zc - 0.8, zc + 0.8))
# grille recess + slats
hood = hood.cut(box(-GRILLE_W, GRILLE_W, -9.3, 13.8, HOOD_Z1 - 2.6, 245))
slat_ys = [-7.5, -3.6, 0.3, 4.2, 8.1, 12.0]
for ys in slat_ys:
    hood = hood.union(box(-GRILLE_W, GRILLE_W, ys - 0.9, ys + 0.9, HOOD_Z1 - 2.6, HOOD_Z1 - 0.8))
# two air-intake slots on the nose, just above the grille
for s in (1, -1):
    v0, v1 = (3.0, 12.0) if s > 0 else (-12.0, -3.0)
    hood = hood.cut(box(v0, v1, 16.8, 18.2, HOOD_Z1 - 7.5, HOOD_Z1 + 5))
# "V" notch of the grille surround (emblem seat)
hood = hood.union(cq.Workplane("XY").workplane(offset=HOOD_Z1 - 2.7)
                  .polyline([(-5.0, 13.9), (5.0, 13.9), (0.0, 9.2)]).close().extrude(2.6))
# headlights (lens blocks on the fender noses)
for s in (1, -1):
    l0, l1 = (23.5, 33.5) if s > 0 else (-33.5, -23.5)
    hood = hood.union(box(l0, l1, -7.0, -2.5, 224.0, 228.6))
parts.append(hood)

# front leaf springs under the rails
for s in (1, -1):
    q0, q1 = (FRAIL_X0, FRAIL_X1) if s > 0 else (-FRAIL_X1, -FRAIL_X0)
    parts.append(box(q0, q1, -15.2, RAIL_Y0, 188.0, 229.0))

# ------------------------------------------------------------------
# front bumper (bent plate with wrap-around ends)
# ------------------------------------------------------------------
bump = (cq.Workplane("XZ").workplane(offset=-BUMP_Y1)
        .polyline([(-35.7, 231.0), (-22.9, BUMP_ZF), (22.9, BUMP_ZF), (35.7, 231.0),
                   (35.7, 228.0), (22.9, BUMP_ZF - 3.2), (-22.9, BUMP_ZF - 3.2), (-35.7, 228.0)])
        .close().extrude(BUMP_Y1 - BUMP_Y0))
for s in (1, -1):
    h0, h1 = (8.3, 15.3) if s > 0 else (-15.3, -8.3)
    bump = bump.cut(box(h0, h1, -17.4, -12.1, BUMP_ZF - 1.2, BUMP_ZF + 1))
parts.append(bump)

# ------------------------------------------------------------------
_solids = []
for _p in parts:
    _solids += _p.solids().vals()
result = cq.Workplane("XY").add(_solids[0].fuse(*_solids[1:]).clean())
